import math

import cadquery as cq

# camera used for the main reference picture (default)
VIEW = {"azimuth": 45, "elevation": 26}

# Tray lid / card-guide plate:
#   square plate with rounded corners, raised perimeter rim and a recessed floor,
#   four card-guide bands (two thin walls + ledges + centre channel) along X,
#   three locating pins, two square sockets, four U-shaped screw bosses on the rim,
#   a slot in the rim, two latch tabs on the side rims and an engraved logo underneath.

# ---------------- driving dimensions (mm) ----------------
S = 200.0          # plate outer size (square)
R = 19.5           # outer corner radius
H = 8.0            # rim top height (overall plate thickness)
RIM = 3.6          # rim wall width
F = 3.5            # floor top height (floor thickness)
RIM_FIL = 0.0      # fillet between rim inner face and floor (0 = sharp)

# bands (card guides) running along X
N_BAND = 4
BAND_L = 172.0
BAND_W = 26.2
BAND_Y0 = 48.6     # centre Y of first (back) band
BAND_PITCH = 41.4
Z_CHAN = 8.3       # channel top
Z_LEDGE = 9.5      # ledge top
Z_WALL = 13.0      # wall top
WALL_T = 1.2
LEDGE_W = 5.1
NOTCH_W = 6.0
NOTCH_D = 1.0
NOTCH_X = [-64.0, -20.0, 24.0, 68.0]

# pins between bands
PIN_X = 1.2
PIN_D = 5.5
PIN_TOP = 21.2

# square blocks near back edge
BLK_SX = 12.6
BLK_SY = 13.5
BLK_TOP = 12.4
BLK_X = [-63.4, -19.2]
BLK_Y = 80.4
BLK_POCKET_X = 10.4
BLK_POCKET_Y = 8.0
BLK_POCKET_D = 2.0
BLK_POCKET_TAPER = 15.0

# screw bosses on the rim (U-shaped, hole slightly offset in X)
BOSS_W_RIM = 12.8   # boss width where it meets the rim
BOSS_W_TIP = 9.6    # boss width at its free end
BOSS_DEPTH = 8.0    # how far the boss protrudes from the rim inner face
BOSS_FR = 4.0       # fillet of the free-end corners
BOSS_TOP = 9.0
# (hole x, boss body x, side, hole offset from rim inner face)
BOSSES = [(-41.0, -39.9, 1, 4.4), (69.9, 70.5, 1, 4.4),
          (-41.6, -40.5, -1, 3.4), (46.1, 47.0, -1, 3.4)]
HOLE_D = 2.0
CBORE_D = 6.2
CBORE_DEPTH = 1.5
STEP_D = 3.4
STEP_DEPTH = 3.5
BOT_CBORE_D = 6.0   # counterbore from the underside
BOT_CBORE_DEPTH = 3.0

# rim notch (back-left)
RNOTCH_X = -74.2
RNOTCH_W = 3.8
RNOTCH_Z = 1.0

# side latch tabs
TAB_Y = -13.8
TAB_L = 18.6
TAB_T = 3.0
TAB_TOP = 7.5

# underside logo: engraved V-shaped grooves (polylines in XY on the bottom face)
LOGO_W = 2.4
LOGO_D = 0.5
LOGO_PATHS = [
    [(-68.5, 45.5), (-26.0, -44.5), (5.6, 25.5)],
    [(-53.2, 45.7), (-26.2, -13.1), (-1.0, 40.0)],
    [(10.8, 16.0), (31.2, -30.4), (67.4, 44.6)],
    [(25.5, -7.5), (30.5, -18.6), (53.6, 43.7)],
    [(23.6, -45.7), (2.4, 2.4)],
]

# ---------------- base plate with pocket ----------------
plate = (cq.Workplane("XY")
         .sketch().rect(S, S).vertices().fillet(R).finalize()
         .extrude(H))
pocket = (cq.Workplane("XY").workplane(offset=F)
          .sketch().rect(S - 2 * RIM, S - 2 * RIM).vertices().fillet(R - RIM).finalize()
          .extrude(H - F + 1))
if RIM_FIL > 0:
    pocket = pocket.faces("<Z").edges().fillet(RIM_FIL)
body = plate.cut(pocket)


def box(cx, cy, z0, lx, ly, h):
    return cq.Workplane("XY").box(lx, ly, h, centered=(True, True, False)).translate((cx, cy, z0))


# ---------------- bands ----------------
for i in range(N_BAND):
    yc = BAND_Y0 - i * BAND_PITCH
    band = box(0, yc, F - 0.01, BAND_L, BAND_W, Z_CHAN - F + 0.01)
    for s in (1, -1):
        yl = yc + s * (BAND_W / 2 - WALL_T - LEDGE_W / 2)
        band = band.union(box(0, yl, Z_CHAN - 0.01, BAND_L, LEDGE_W + 0.02, Z_LEDGE - Z_CHAN + 0.01))
        yw = yc + s * (BAND_W / 2 - WALL_T / 2)
        wall = box(0, yw, F - 0.01, BAND_L, WALL_T, Z_WALL - F + 0.01)
        if s > 0:  # only the back (+Y) wall of each band carries the notches
            for nx in NOTCH_X:
                wall = wall.cut(box(nx, yw, Z_WALL - NOTCH_D, NOTCH_W, WALL_T + 1, NOTCH_D + 1))
        band = band.union(wall)
    body = body.union(band)

# ---------------- pins ----------------
for i in range(N_BAND - 1):
    yp = BAND_Y0 - (i + 0.5) * BAND_PITCH
    pin = (cq.Workplane("XY").workplane(offset=F - 0.01)
           .center(PIN_X, yp).circle(PIN_D / 2).extrude(PIN_TOP - F + 0.01))
    body = body.union(pin)

# ---------------- blocks ----------------
for bx in BLK_X:
    blk = box(bx, BLK_Y, F - 0.01, BLK_SX, BLK_SY, BLK_TOP - F + 0.01)
    pk = (cq.Workplane("XY").workplane(offset=BLK_TOP).center(bx, BLK_Y)
          .rect(BLK_POCKET_X, BLK_POCKET_Y).extrude(-BLK_POCKET_D, taper=BLK_POCKET_TAPER))
    blk = blk.cut(pk)
    body = body.union(blk)

# ---------------- bosses ----------------
inner = S / 2 - RIM
for (hx, bx, sd, hoff) in BOSSES:
    y_rim = sd * (inner + 0.01)
    y_tip = sd * (inner - BOSS_DEPTH)
    pts = [(bx - BOSS_W_RIM / 2, y_rim), (bx + BOSS_W_RIM / 2, y_rim),
           (bx + BOSS_W_TIP / 2, y_tip), (bx - BOSS_W_TIP / 2, y_tip)]
    boss = (cq.Workplane("XY").workplane(offset=F - 0.01)
            .polyline(pts).close().extrude(BOSS_TOP - F + 0.01))
    sel = ">Y" if sd < 0 else "<Y"
    boss = boss.edges("|Z").edges(sel).fillet(BOSS_FR)
    body = body.union(boss)
for (hx, bx, sd, hoff) in BOSSES:
    hy = sd * (inner - hoff)
    hole = cq.Workplane("XY").workplane(offset=-1).center(hx, hy).circle(HOLE_D / 2).extrude(BOSS_TOP + 2)
    stp = (cq.Workplane("XY").workplane(offset=BOSS_TOP - STEP_DEPTH)
           .center(hx, hy).circle(STEP_D / 2).extrude(STEP_DEPTH + 1))
    cb = (cq.Workplane("XY").workplane(offset=BOSS_TOP - CBORE_DEPTH)
          .center(hx, hy).circle(CBORE_D / 2).extrude(CBORE_DEPTH + 1))
    bcb = (cq.Workplane("XY").workplane(offset=-1)
           .center(hx, hy).circle(BOT_CBORE_D / 2).extrude(BOT_CBORE_DEPTH + 1))
    body = body.cut(hole).cut(stp).cut(cb).cut(bcb)

# ---------------- rim notch ----------------
body = body.cut(box(RNOTCH_X, S / 2 - RIM / 2 + 0.5, RNOTCH_Z, RNOTCH_W, RIM + 1.0, H))

# ---------------- side tabs ----------------
for s in (1, -1):
    tx = s * (inner - TAB_T / 2 + 0.25)
    body = body.union(box(tx, TAB_Y, F - 0.01, TAB_T + 0.5, TAB_L, TAB_TOP - F + 0.01))

# ---------------- underside logo ----------------
logo = None
for path in LOGO_PATHS:
    nseg = len(path) - 1
    for k, ((x0, y0), (x1, y1)) in enumerate(zip(path[:-1], path[1:])):
        L = math.hypot(x1 - x0, y1 - y0)
        ux, uy = (x1 - x0) / L, (y1 - y0) / L
        e0 = LOGO_W / 2 if k > 0 else 0.0          # extend into the joints only
        e1 = LOGO_W / 2 if k < nseg - 1 else 0.0
        ax, ay = x0 - ux * e0, y0 - uy * e0
        bx_, by_ = x1 + ux * e1, y1 + uy * e1
        Lx = L + e0 + e1
        ang = math.degrees(math.atan2(uy, ux))
        seg = (cq.Workplane("XY").box(Lx, LOGO_W, LOGO_D + 1, centered=(True, True, False))
               .rotate((0, 0, 0), (0, 0, 1), ang)
               .translate(((ax + bx_) / 2, (ay + by_) / 2, -1)))
        logo = seg if logo is None else logo.union(seg)
body = body.cut(logo)

result = body
